"""Sheet-metal 'pinwheel' motor bracket.

A flat plate (in the XZ plane, front face at y = 0) with a large central bore and an
8-hole bolt circle.  The plate has four identical lobes arranged with 4-fold rotational
symmetry about the Y axis.  Each lobe has one straight edge along which a mounting tab is
bent 90 deg backwards (+Y) with a small inside bend radius.  Every tab carries two large
holes plus a pattern of small holes and has rounded far corners.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
T = 1.7               # sheet thickness
RB = 3.3              # inside bend radius
OFF = RB + T          # offset of a tab's outer face from the bore centre line

LOBE_OUT = 119.0      # reach of each lobe along its own axis (from bore centre)
LOBE_SIDE = 71.5      # lateral reach of each lobe
CORNER_R = 66.0       # big rounded outer corner of each lobe

CENTER_HOLE_D = 106.0 # central bore
BOLT_BC_D = 132.3     # bolt circle diameter
BOLT_D = 7.0          # bolt hole diameter
BOLT_N = 8
BOLT_START = 30.0     # deg, first bolt hole (measured from +X toward +Z)

TAB_L = 93.0          # tab reach in +Y, measured from the plate front face
RELIEF = 1.5          # bend relief between the tab and the neighbouring lobe
TAB_Z0 = LOBE_SIDE + RELIEF   # inner edge of the tab (along the lobe axis)
TAB_Z1 = LOBE_OUT             # outer edge of the tab
TAB_W = TAB_Z1 - TAB_Z0
TAB_CORNER_R = 6.0    # rounded far corners of the tab

BIG_D = 20.0                  # two large holes in every tab
BIG_U = (31.5, 73.1)          # their distance from the plate front face
SMALL_D = 2.85                # small holes in every tab
SQ = 13.0                     # half pitch of the 4-hole square around each large hole
ROW_DU = -21.0                # row of three small holes, offset from each large hole
ROW_V = 15.2                  # pitch inside the row of three


def lobe_flat():
    """Flat part of the 'top' lobe: x in [0, LOBE_SIDE], plate at y in [0, T]."""
    cx = LOBE_SIDE - CORNER_R
    cz = LOBE_OUT - CORNER_R
    a = math.radians(45.0)
    mid = (cx + CORNER_R * math.cos(a), cz + CORNER_R * math.sin(a))
    return (
        cq.Workplane("XZ")
        .moveTo(0, -OFF)
        .lineTo(LOBE_SIDE, -OFF)
        .lineTo(LOBE_SIDE, cz)
        .threePointArc(mid, (cx, LOBE_OUT))
        .lineTo(0, LOBE_OUT)
        .close()
        .extrude(-T)          # XZ normal is -Y, so a negative distance goes to +Y
    )


def lobe_bend():
    """90 deg bend (quarter annulus about an axis parallel to Z at x=0, y=T+RB)."""
    yc = T + RB
    s = math.sin(math.radians(45.0))
    return (
        cq.Workplane("XY", origin=(0, 0, TAB_Z0))
        .moveTo(0, 0)
        .threePointArc((-OFF * s, yc - OFF * s), (-OFF, yc))
        .lineTo(-RB, yc)
        .threePointArc((-RB * s, yc - RB * s), (0, T))
        .close()
        .extrude(TAB_W)
    )


def lobe_tab():
    """Flat tab in a YZ plane at x in [-OFF, -RB], reaching back to y = TAB_L."""
    yc = T + RB
    flat_len = TAB_L - yc
    tab = (
        cq.Workplane("YZ", origin=(-OFF, 0, 0))
        .center(yc + flat_len / 2.0, (TAB_Z0 + TAB_Z1) / 2.0)
        .rect(flat_len, TAB_W)
        .extrude(T)
    )
    return tab.edges("|X").edges(">Y").fillet(TAB_CORNER_R)


def tab_hole_cutter():
    """Cylinders for the tab hole pattern (positions as (u along Y, v along Z))."""
    vmid = (TAB_Z0 + TAB_Z1) / 2.0
    big = [(u, vmid) for u in BIG_U]
    small = []
    for u in BIG_U:
        for du in (-SQ, SQ):
            for dv in (-SQ, SQ):
                small.append((u + du, vmid + dv))
        for dv in (-ROW_V, 0.0, ROW_V):
            small.append((u + ROW_DU, vmid + dv))
    wp = cq.Workplane("YZ", origin=(-OFF - 1.0, 0, 0))
    c_big = wp.pushPoints(big).circle(BIG_D / 2.0).extrude(T + 2.0)
    c_small = wp.pushPoints(small).circle(SMALL_D / 2.0).extrude(T + 2.0)
    return c_big.union(c_small)


def one_lobe():
    bent = lobe_bend().union(lobe_tab()).cut(tab_hole_cutter())
    return lobe_flat().union(bent)


# four lobes, rotated about the bore axis (+Y) in 90 deg steps
lobe = one_lobe()
part = lobe
for k in range(1, 4):
    part = part.union(lobe.rotate((0, 0, 0), (0, 1, 0), 90.0 * k))

# central bore and bolt circle through the plate
plate_cut = (
    cq.Workplane("XZ", origin=(0, T + 1.0, 0))
    .circle(CENTER_HOLE_D / 2.0)
    .extrude(T + 2.0)
)
bolts = (
    cq.Workplane("XZ", origin=(0, T + 1.0, 0))
    .polarArray(BOLT_BC_D / 2.0, BOLT_START, 360.0, BOLT_N)
    .circle(BOLT_D / 2.0)
    .extrude(T + 2.0)
)

result = part.cut(plate_cut).cut(bolts)

VIEW = {"azimuth": 45, "elevation": 26}
